import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT_FRONT = 30.0     # outer radius of the arms at the front face
R_OUT_BACK = 24.1      # outer radius of the arms at the back end
WALL_FRONT = 7.15      # radial wall thickness of the arms at the front
WALL_BACK = 7.1        # radial wall thickness of the arms at the tips
R_DISC = R_OUT_FRONT - WALL_FRONT   # disc radius (= arm inner radius at front)
R_IN_BACK = R_OUT_BACK - WALL_BACK
LENGTH = 38.3          # overall axial length (front face -> arm tips)
DISC_T = 6.9           # thickness of the front disc
PROFILE_SAG = 0.7      # outward bulge of the (slightly curved) arm profile

N_ARMS = 3
ARM_SPAN = 60.0        # angular width of each arm (deg)
ARM_CENTER0 = 90.0     # first arm centred on +Z

TRI_SIDE = 18.4        # side of the triangular through hole
TRI_CHAMFER = 1.4      # chamfer on the front edge of the triangle

VIEW = {"azimuth": 45, "elevation": 26}


def arc_mid(p0, p1, sag):
    """midpoint of an arc from p0 to p1 bulging by `sag` to the outside (+r)."""
    mx, my = (p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    ln = math.hypot(dx, dy)
    nx, ny = dy / ln, -dx / ln          # normal pointing to +r for a run toward +y
    if nx < 0:
        nx, ny = -nx, -ny
    return (mx + nx * sag, my + ny * sag)


# ---------------- revolved bodies (axis = Y, front face at y = 0) ----------------
po0 = (R_OUT_FRONT, 0.0)
po1 = (R_OUT_BACK, LENGTH)
pi0 = (R_DISC, 0.0)
pi1 = (R_IN_BACK, LENGTH)

# solid bounded by the outer (slightly curved) arm profile
outer_solid = (
    cq.Workplane("XY")
    .moveTo(0.0, 0.0)
    .lineTo(*po0)
    .threePointArc(arc_mid(po0, po1, PROFILE_SAG), po1)
    .lineTo(0.0, LENGTH)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)
# solid bounded by the inner arm profile (bore of the arms)
inner_solid = (
    cq.Workplane("XY")
    .moveTo(0.0, 0.0)
    .lineTo(*pi0)
    .threePointArc(arc_mid(pi0, pi1, PROFILE_SAG), pi1)
    .lineTo(0.0, LENGTH)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)
shell = outer_solid.cut(inner_solid)

# ---------------- angular sectors that keep the three arms ----------------
RB = 3.0 * R_OUT_FRONT
sectors = None
for k in range(N_ARMS):
    c = math.radians(ARM_CENTER0 + k * 360.0 / N_ARMS)
    h = math.radians(ARM_SPAN / 2.0)
    pts = [
        (0.0, 0.0),
        (RB * math.cos(c - h), RB * math.sin(c - h)),
        (RB * math.cos(c), RB * math.sin(c)),
        (RB * math.cos(c + h), RB * math.sin(c + h)),
    ]
    # XZ workplane: local x = X, local y = Z, normal = -Y  -> extrude(-d) goes to +Y
    w = cq.Workplane("XZ").workplane(offset=1.0).polyline(pts).close().extrude(-(LENGTH + 2.0))
    sectors = w if sectors is None else sectors.union(w)

arms = shell.intersect(sectors)

# ---------------- front disc: the bore solid cut to the disc thickness ----------------
slab = cq.Workplane("XZ").rect(4 * R_OUT_FRONT, 4 * R_OUT_FRONT).extrude(-DISC_T)
disc = inner_solid.intersect(slab)

body = arms.union(disc)

# ---------------- triangular through hole with chamfered front edge ----------------
rc = TRI_SIDE / math.sqrt(3.0)  # circumradius
tri = [(rc * math.cos(math.radians(90 + 120 * i)), rc * math.sin(math.radians(90 + 120 * i))) for i in range(3)]
hole = cq.Workplane("XZ").workplane(offset=1.0).polyline(tri).close().extrude(-(DISC_T + 2.0))
body = body.cut(hole)

body = body.edges(
    cq.selectors.BoxSelector((-R_DISC * 0.6, -0.05, -R_DISC * 0.6), (R_DISC * 0.6, 0.05, R_DISC * 0.6))
).chamfer(TRI_CHAMFER)

result = body
